import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# lens-shaped front profile (three arcs), points in (X, Z); front face lies in Y = 0
P_LEFT = (0.0, 11.2)
P_TOP = (34.8, 60.5)
P_R1 = (100.0, 32.1)
P_R2 = (98.4, 24.2)
P_BOT = (43.6, 0.0)
C_UL = (85.08, -11.0)     # centre of upper-left arc
C_TR = (36.71, -22.43)    # centre of top-right arc
R_TR = 83.24
C_BT = (41.51, 80.22)     # centre of bottom arc
R_BT = 80.51

# smooth ellipsoidal dome on the back
DOME_C = (42.0, -1.0, 34.0)
DOME_AX = (36.0, 31.0, 31.0)

# fluted fan radiating from the "umbo" (top corner)
UMBO = (35.9, 61.4)
# base surface of the fan: (rho, depth Y)
BASE_PROFILE = [(16.0, 10.0), (24.0, 28.0), (40.0, 32.5), (60.0, 33.8), (95.0, 34.2)]
# cap limiting the rib crests: (rho, depth Y)
CAP_PROFILE = [(0.0, 45.0), (52.0, 45.0), (57.6, 37.3), (95.0, 37.4)]
RIB_ANGLES = [-27.5, -50.0, -73.5, -95.0, -117.5]   # rib directions about the umbo (deg, in XZ)
# convex rib cone: (rho, axis depth Y, radius) at its start / at the rim
RIB_A = (10.0, 25.5, 0.3)
RIB_B = (57.6, 32.9, 4.5)
RIB_DY = [0.0, -2.0, 0.0, 0.0, -1.5]          # per-rib depth offset (outer ribs sit lower)
RIB_RHO0 = [38.0, 10.0, 10.0, 10.0, 10.0]     # where each rib starts (the one next to the top-right edge starts late)
FLUTE_ANGLES = [(a + b) / 2 for a, b in zip(RIB_ANGLES, RIB_ANGLES[1:])]
FL_A = (24.0, 29.2, 3.0)                      # concave flute cone: (rho, axis depth Y, radius) inner end
FL_B = (57.6, 34.4, 6.0)                      # ... at the rim
RHO_END = 95.0
FL_RHO0 = 14.0                                # flutes start inside the base

TR_STRAIGHT = 15.5        # top-right edge stays straight this far back
# relief behind the top-right band: lofted ruled surface; its inward run per 10 mm of depth
TR_RUN_MID = 10.0         # near the umbo / middle of the arc
TR_RUN_END = 4.5          # at the right end
TR_PHI = (98.0, 67.0, 36.0)   # angles (deg, about the top-right arc centre) spanned by the relief
SHELF_Y = 25.5           # depth limit of the fan near the top-right edge
SHELF_W = 16.0           # width of that zone, measured in from the top-right arc
END_X, END_Y = 82.0, 25.8   # the right-end portion of the fan is no deeper than END_Y
R_UL = 87.57
UL_STRAIGHT = 22.5        # upper-left edge stays straight this far back, then the fan drops away
UL_RUN = 5.0              # inward run of the relief per 10 mm of depth
UL_PHI = (162.0, 140.0, 120.0)   # angles (deg, about the upper-left arc centre) spanned by the relief
BT_STRAIGHT = 14.2        # bottom stays straight this far back
BT_ROUND = 60.0           # large round on the bottom back edge


def revolve_profile(cmds, center):
    """cmds in (radial, Y) coords; revolved about an axis parallel to Y through center=(X,Z)."""
    wp = cq.Workplane("XY").moveTo(*cmds[0][1])
    for c in cmds[1:]:
        if c[0] == "l":
            wp = wp.lineTo(*c[1])
        else:
            wp = wp.threePointArc(c[1], c[2])
    s = wp.close().revolve(360, (0, 0, 0), (0, 1, 0))
    return s.translate((center[0], 0, center[1]))


def arc_pts(c, r, a0, a1):
    am = (a0 + a1) / 2
    return ((c[0] + r * math.cos(am), c[1] + r * math.sin(am)),
            (c[0] + r * math.cos(a1), c[1] + r * math.sin(a1)))


def arc_mid(c, p, q):
    r = math.hypot(p[0] - c[0], p[1] - c[1])
    a1 = math.atan2(p[1] - c[1], p[0] - c[0])
    a2 = math.atan2(q[1] - c[1], q[0] - c[0])
    da = (a2 - a1 + math.pi) % (2 * math.pi) - math.pi
    am = a1 + da / 2
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


# --- lens extrusion (front face at Y=0, extends to +Y) ---
lens = (
    cq.Workplane("XZ")
    .moveTo(*P_LEFT)
    .threePointArc(arc_mid(C_UL, P_LEFT, P_TOP), P_TOP)
    .threePointArc(arc_mid(C_TR, P_TOP, P_R1), P_R1)
    .lineTo(*P_R2)
    .threePointArc(P_BOT, P_LEFT)
    .close()
    .extrude(-60.0)
)


# --- ellipsoidal dome ---
def ellipsoid(c, ax):
    return cq.Workplane("XY").add(
        cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
        .transformGeometry(cq.Matrix([[ax[0], 0, 0, c[0]],
                                      [0, ax[1], 0, c[1]],
                                      [0, 0, ax[2], c[2]]]))
    )


dome = ellipsoid(DOME_C, DOME_AX)


# --- fan radiating from the umbo: base surface + convex ribs + concave flutes ---
def profile_solid(prof, y_floor=-1.0):
    cmds = [("s", (0, y_floor))]
    if prof[0][0] > 0.0:
        cmds.append(("l", (prof[0][0], y_floor)))
    cmds += [("l", p) for p in prof]
    cmds.append(("l", (prof[-1][0], y_floor)))
    return revolve_profile(cmds, UMBO)


base = profile_solid(BASE_PROFILE)
cap = profile_solid(CAP_PROFILE)


def radial_cone(angle, a, b, rho0, rho1=RHO_END):
    """cone along the radial line at `angle` about the umbo, linear between a and b,
    spanning rho0..rho1 (extrapolated)."""
    def at(rho):
        f = (rho - a[0]) / (b[0] - a[0])
        return (a[1] + f * (b[1] - a[1]), a[2] + f * (b[2] - a[2]))

    t = math.radians(angle)
    (y0, r0), (y1, r1) = at(rho0), at(rho1)
    p0 = cq.Vector(UMBO[0] + rho0 * math.cos(t), y0, UMBO[1] + rho0 * math.sin(t))
    p1 = cq.Vector(UMBO[0] + rho1 * math.cos(t), y1, UMBO[1] + rho1 * math.sin(t))
    d = p1 - p0
    return cq.Solid.makeCone(r0, r1, d.Length, p0, d.normalized())


ribs = None
for a, dy, r0 in zip(RIB_ANGLES, RIB_DY, RIB_RHO0):
    pa, pb = [(p[0], p[1] + dy, p[2]) for p in (RIB_A, RIB_B)]
    if r0 > pa[0]:
        pa = (r0 - 8.0, pa[1] + (pb[1] - pa[1]) * (r0 - 8.0 - pa[0]) / (pb[0] - pa[0]), 0.3)
    c = radial_cone(a, pa, pb, pa[0])
    ribs = c if ribs is None else ribs.fuse(c)
fan = base.union(cq.Workplane("XY").add(ribs).intersect(cap))
for a in FLUTE_ANGLES:
    fan = fan.cut(cq.Workplane("XY").add(radial_cone(a, FL_A, FL_B, FL_RHO0)))

# --- ruled reliefs behind the arc edges of the lens ---
def relief_cut(center=C_TR, radius=R_TR, y0=TR_STRAIGHT, phis=TR_PHI,
               runs=(TR_RUN_MID, TR_RUN_MID, TR_RUN_END)):
    """ruled (lofted) relief behind an arc edge of the lens: everything outside the sloped
    surface starting at depth y0 on the arc is removed."""
    y1 = y0 + 34.5
    k = (y1 - y0) / 10.0

    def pt(phi, r):
        a = math.radians(phi)
        return (center[0] + r * math.cos(a), center[1] + r * math.sin(a))

    pa, pm, pb = phis
    ro = radius + 15.0
    w = cq.Workplane("XZ", origin=(0, y0, 0))
    w = (w.moveTo(*pt(pa, radius)).threePointArc(pt(pm, radius), pt(pb, radius))
          .lineTo(*pt(pb, ro)).threePointArc(pt(pm, ro), pt(pa, ro)).close())
    ri = [radius - r * k for r in runs]
    w = w.workplane(offset=-(y1 - y0))
    w = (w.moveTo(*pt(pa, ri[0])).threePointArc(pt(pm, ri[1]), pt(pb, ri[2]))
          .lineTo(*pt(pb, ro)).threePointArc(pt(pm, ro), pt(pa, ro)).close())
    return w.loft(ruled=True)


# --- round on the bottom back edge (about the bottom arc axis) ---
c3 = (R_BT - BT_ROUND, BT_STRAIGHT)
a_end = math.asin(min(1.0, (50.0 - BT_STRAIGHT) / BT_ROUND))
m3, e3 = arc_pts(c3, BT_ROUND, 0.0, a_end)
env_bt = revolve_profile(
    [("s", (0, -1)), ("l", (R_BT + 0.01, -1)), ("l", (R_BT + 0.01, BT_STRAIGHT)), ("a", m3, e3),
     ("l", (0, e3[1]))],
    C_BT,
)

env_shelf = revolve_profile(
    [("s", (0, -1)), ("l", (R_TR + 0.01, -1)), ("l", (R_TR + 0.01, SHELF_Y)),
     ("l", (R_TR - SHELF_W, SHELF_Y)), ("l", (R_TR - SHELF_W - 3.0, SHELF_Y + 25.0)),
     ("l", (0, SHELF_Y + 25.0))],
    C_TR,
)
end_cut = cq.Workplane("XY").box(60, 60, 120, centered=False).translate((END_X, END_Y, -30))
tr_cut = relief_cut()
ul_cut = relief_cut(C_UL, R_UL, UL_STRAIGHT, UL_PHI, (0.5, UL_RUN, UL_RUN))

# --- assemble: dome + trimmed fan, clipped by the lens prism and the bottom round ---
fan = fan.cut(tr_cut).cut(ul_cut).cut(end_cut).intersect(env_shelf)
body = lens.intersect(dome.union(fan)).intersect(env_bt)

result = body
